import math
import cadquery as cq

# ============================================================================
# Curved-back slatted tray / pallet segment
#   - flat plate with fine slats (grooves) along X, fork pockets on 3 sides
#   - tall curved "scoop" wall along the front (-Y) edge, slightly bowed in plan
#   - stiffening ribs on the concave face, an ear at the -X end
# ============================================================================

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # length along X
DEPTH = 93.8       # overall depth along Y (wall outer face -> back edge)
T_PLATE = 10.9     # plate thickness
H_WALL = 41.7      # wall top height

# wall cross-section: arcs about (CY, CZ) in the YZ plane
CY, CZ = 74.5, 46.7
R_OUT = 74.36      # convex outer face
R_IN = 68.9        # concave inner face (upper smooth part)
R_RIB_IN = 64.5    # inner edge of the stiffening ribs
R_RIB_OUT = 70.5   # rib root (buried inside the wall)

# facet heights on the lower part of the outer face
OUT_FACETS = [21.6, 15.6, 9.8, 6.1]
# lower part of the concave face
IN_ARC_Z = 22.0                                 # inner arc ends here
IN_FACET_PTS = [(12.3, 15.5), (14.3, T_PLATE)]  # lower inner facets (Y, Z)

# slight bow of the wall in plan (sagitta at the ends, relative to the middle)
BOW = 1.2

# ribs
RIB_W = 6.0
RIB_X = [30.0, 58.3, 86.6]
END_RIB_W = 4.5
RIB_PEAK = 0.35    # rib ramp peak above wall top

# ear at the -X end of the wall
EAR_W = 7.5
EAR_H = 10.8

# plate grooves (slats)
GROOVE_EDGE = 2.85  # first groove from the back edge
GROOVE_PITCH = 5.554
GROOVE_N = 14
GROOVE_W = 0.35
GROOVE_D = 0.5
GROOVE_X0 = 3.3

# fork-pocket windows
WIN_W = 11.2
WIN_Z0 = 1.95
WIN_H = 5.6
WIN_DEPTH = 20.0
WIN_Y_SIDE = 60.0
WIN_X_BACK = 53.4

# corner notch at +X/+Y
NOTCH_R = 4.0
NOTCH_Z = 3.5

# ---------------- helpers ----------------
z_top = H_WALL
AXIS_Y = ((L / 2.0) ** 2 + BOW ** 2) / (2.0 * BOW)   # bow radius (vertical axis)
BOW_ANG = math.degrees(math.asin((L / 2.0 + 4.0) / AXIS_Y))


def y_on(r, z):
    """Y coordinate of the arc of radius r (about CY,CZ) at height z (front side)."""
    return CY - math.sqrt(r * r - (CZ - z) ** 2)


def arc_mid(r, z0, z1):
    zm = 0.5 * (z0 + z1)
    return (y_on(r, zm), zm)


def prof_wp():
    """Workplane on the mid (X = L/2) YZ section: local x = global Y, local y = Z."""
    return cq.Workplane("YZ", origin=(L / 2.0, 0, 0))


def bowed(wp):
    """Sweep a closed YZ profile (drawn at X=L/2) around the far vertical bow axis."""
    solid = wp.revolve(2.0 * BOW_ANG, (AXIS_Y, 0, 0), (AXIS_Y, 1, 0))
    return solid.rotate((L / 2.0, AXIS_Y, 0), (L / 2.0, AXIS_Y, 1), -BOW_ANG)


def slab(x0, x1):
    return (cq.Workplane("XY")
            .box(x1 - x0, 400.0, 400.0, centered=(False, True, True))
            .translate((x0, 0, 0)))


# ---------------- curved wall (with the plate strip next to it) ----------------
# The wall is first made taller than needed (up to the ear tip); everything above
# the wall top except the ear is then trimmed away.
Y_JOIN = 26.0   # wall profile reaches this far into the plate
z_hi = z_top + EAR_H + 1.0
p_out_hi = (y_on(R_OUT, z_hi), z_hi)
p_in_hi = (y_on(R_IN, z_hi), z_hi)

wp = prof_wp().moveTo(*p_out_hi)
z_f0 = OUT_FACETS[0]
wp = wp.threePointArc(arc_mid(R_OUT, z_hi, z_f0), (y_on(R_OUT, z_f0), z_f0))
for zf in OUT_FACETS[1:]:
    wp = wp.lineTo(y_on(R_OUT, zf), zf)
wp = wp.lineTo(y_on(R_OUT, 0.0), 0.0)
wp = wp.lineTo(Y_JOIN, 0.0)
wp = wp.lineTo(Y_JOIN, T_PLATE)
for (fy, fz) in reversed(IN_FACET_PTS):
    wp = wp.lineTo(fy, fz)
wp = wp.lineTo(y_on(R_IN, IN_ARC_Z), IN_ARC_Z)
wp = wp.threePointArc(arc_mid(R_IN, IN_ARC_Z, z_hi), p_in_hi)
wp = wp.close()
wall = bowed(wp).intersect(slab(0.0, L))

# ear at the -X end: keep the part of the over-tall wall under a concave curve
ear_keep = (cq.Workplane("XZ", origin=(0, 20.0, 0))
            .moveTo(-1.0, z_top - 1.0)
            .lineTo(EAR_W, z_top - 1.0)
            .lineTo(EAR_W, z_top)
            .threePointArc((EAR_W * 0.42, z_top + EAR_H * 0.30), (0.0, z_top + EAR_H))
            .lineTo(-1.0, z_top + EAR_H)
            .close()
            .extrude(30.0))
trim = (cq.Workplane("XY")
        .box(L + 2.0, 30.0, EAR_H + 5.0, centered=False)
        .translate((-1.0, -8.0, z_top))
        .cut(ear_keep))
wall = wall.cut(trim)

# ---------------- plate ----------------
plate = (cq.Workplane("XY")
         .box(L, DEPTH - (Y_JOIN - 6.0), T_PLATE, centered=False)
         .translate((0, Y_JOIN - 6.0, 0)))
body = wall.union(plate)

# ---------------- plate grooves (open at +X end) ----------------
for i in range(GROOVE_N):
    gy = DEPTH - GROOVE_EDGE - i * GROOVE_PITCH
    g = (cq.Workplane("XY")
         .box(L - GROOVE_X0 + 1.0, GROOVE_W, GROOVE_D + 1.0, centered=(False, True, False))
         .translate((GROOVE_X0, gy, T_PLATE - GROOVE_D)))
    body = body.cut(g)


# ---------------- ribs on the concave face ----------------
def rib(x0, w):
    """Rib following the concave face; its top is a low ramp peaking at the inner edge."""
    zb = 8.0
    y_root_top = y_on(R_RIB_OUT, z_top)
    z_r = z_top - 1.0
    y_r = y_on(R_RIB_IN, z_r)
    y_pk = y_r - 1.1
    z_pk = z_top + RIB_PEAK
    p = (prof_wp()
         .moveTo(y_root_top, z_top)
         .threePointArc((0.5 * (y_root_top + y_pk), 0.5 * (z_top + z_pk) + 0.12), (y_pk, z_pk))
         .threePointArc((y_r - 0.3, z_top - 0.05), (y_r, z_r))
         .threePointArc(arc_mid(R_RIB_IN, z_r, zb), (y_on(R_RIB_IN, zb), zb))
         .lineTo(y_on(R_RIB_OUT, zb), zb)
         .threePointArc(arc_mid(R_RIB_OUT, zb, z_top), (y_root_top, z_top))
         .close())
    return bowed(p).intersect(slab(x0, x0 + w))


for rx in RIB_X:
    body = body.union(rib(rx - RIB_W / 2.0, RIB_W))
body = body.union(rib(0.0, END_RIB_W))

# ---------------- fork pockets ----------------
win_px = (cq.Workplane("XY")                      # +X face
          .box(WIN_DEPTH + 1.0, WIN_W, WIN_H, centered=(False, True, False))
          .translate((L - WIN_DEPTH, WIN_Y_SIDE, WIN_Z0)))
win_nx = (cq.Workplane("XY")                      # -X face
          .box(WIN_DEPTH + 1.0, WIN_W, WIN_H, centered=(False, True, False))
          .translate((-1.0, WIN_Y_SIDE, WIN_Z0)))
win_py = (cq.Workplane("XY")                      # +Y face
          .box(WIN_W, WIN_DEPTH + 1.0, WIN_H, centered=(True, False, False))
          .translate((WIN_X_BACK, DEPTH - WIN_DEPTH, WIN_Z0)))
body = body.cut(win_px).cut(win_nx).cut(win_py)

# ---------------- corner notch at +X/+Y ----------------
notch = (cq.Workplane("XY", origin=(L, DEPTH, NOTCH_Z))
         .circle(NOTCH_R).extrude(T_PLATE))
body = body.cut(notch)

# centre the part on X/Y
result = body.translate((-L / 2.0, -DEPTH / 2.0, 0))

VIEW = {"azimuth": 45, "elevation": 26}
